import math
import cadquery as cq

# ================= driving dimensions (mm) =================
# lid rim / skirt
R_RIM = 50.0          # outer radius of the lid rim (sharp tip)
RIM_TIP_Z = 7.2       # height of the rim tip
RIM_BAND_R = 49.3     # top edge of the narrow outer rim band
RIM_BAND_Z = 8.5
R_SKIRT = 46.9        # radius of the lower skirt / spigot
SKIRT_TOP_Z = 4.85    # where the concave undercut meets the skirt
COVE_MID = (47.97, 6.2)   # a point on the concave undercut

# knob / neck
JUNC_R = 6.3          # neck radius at the dome / knob junction
JUNC_Z = 20.45
KNOB_R = 13.9         # knob max radius
KNOB_MAX_Z = 32.95
KNOB_EDGE = (13.25, 34.3)  # where the rounded knob rim meets the top cap
KNOB_TOP_Z = 36.15    # top (centre) of the domed cap
CAP_PTS = [(12.4, 34.72), (11.3, 35.15), (9.1, 35.6), (5.0, 36.02)]   # domed cap (r, z)
CAP_START_TAN = (-1.0, 0.75)

# dome profile (r, z) from the rim band up to the neck (smooth single face)
DOME_PTS = [
    (48.3, 9.38),
    (46.4, 10.25),
    (42.0, 11.15),
    (33.4, 12.68),
    (25.3, 13.95),
    (18.5, 15.1),
    (13.5, 16.15),
    (10.4, 17.15),
    (8.4, 18.1),
    (7.0, 19.2),
]
DOME_START_TAN = (-1.0, 0.95)   # dome direction leaving the rim band edge
DOME_END_TAN = (-0.5, 0.87)     # dome arrives at the neck crease ~30 deg off vertical
KNOB_START_TAN = (0.1, 1.0)     # knob flank leaves the neck almost vertically
# knob flank (r, z) from the neck up to the widest point (S-curve, single face)
KNOB_PTS = [
    (6.45, 22.0),
    (6.95, 23.2),
    (7.75, 24.45),
    (8.75, 25.65),
    (10.05, 27.2),
    (11.69, 28.75),
    (12.82, 29.95),
    (13.6, 31.2),
]

# hanging loop (lies in the XZ plane)
LOOP_A_OUT = 9.07     # outer half width
LOOP_B_OUT = 10.77    # outer arch height (half ellipse)
LOOP_A_IN = 5.0       # inner half width
LOOP_B_IN = 5.6       # inner arch height
LOOP_TOP_Z = 47.8     # outer top
LOOP_IN_TOP_Z = 44.05 # inner top
LOOP_T = 3.55         # thickness along Y

# locking tabs on the skirt
TAB_W = 10.7          # tangential width
TAB_H = 3.25          # height (from the bottom face)
TAB_OUT = 48.7        # radial position of the flat outer face
N_TABS = 4

SEAM_ANGLE = 135.0    # rotate revolved body so its seam sits at the back-left


# ================= revolved lid body =================
P_band = (RIM_BAND_R, RIM_BAND_Z)
J = (JUNC_R, JUNC_Z)
W = (KNOB_R, KNOB_MAX_Z)

# rounded knob rim: arc from the widest point (vertical tangent) to the cap edge
_dx, _dz = KNOB_EDGE[0] - W[0], KNOB_EDGE[1] - W[1]
_rk = (_dx * _dx + _dz * _dz) / (-2.0 * _dx)     # centre at (W0 - rk, W1)
_ck = (W[0] - _rk, W[1])
_a1 = math.atan2(KNOB_EDGE[1] - _ck[1], KNOB_EDGE[0] - _ck[0])
KNOB_RIM_MID = (_ck[0] + _rk * math.cos(0.5 * _a1), _ck[1] + _rk * math.sin(0.5 * _a1))


def _chord_params(pts):
    """cumulative chord length parameters (so unit tangents are consistent)"""
    out = [0.0]
    for (x0, y0), (x1, y1) in zip(pts[:-1], pts[1:]):
        out.append(out[-1] + math.hypot(x1 - x0, y1 - y0))
    return out


def _unit(v):
    l = math.hypot(v[0], v[1])
    return (v[0] / l, v[1] / l)


dome_all = [P_band] + DOME_PTS + [J]
knob_all = [J] + KNOB_PTS + [W]
cap_all = [KNOB_EDGE] + CAP_PTS + [(0.0, KNOB_TOP_Z)]

prof = (
    cq.Workplane("XZ")
    .moveTo(0, 0)
    .lineTo(R_SKIRT, 0)
    .lineTo(R_SKIRT, SKIRT_TOP_Z)
    .threePointArc(COVE_MID, (R_RIM, RIM_TIP_Z))
    .threePointArc((R_RIM - 0.22, 0.5 * (RIM_TIP_Z + RIM_BAND_Z)), P_band)
    .spline(dome_all[1:], includeCurrent=True, tangents=[_unit(DOME_START_TAN), _unit(DOME_END_TAN)],
            parameters=_chord_params(dome_all), scale=False)
    .spline(knob_all[1:], includeCurrent=True, tangents=[_unit(KNOB_START_TAN), (0.0, 1.0)],
            parameters=_chord_params(knob_all), scale=False)
    .threePointArc(KNOB_RIM_MID, KNOB_EDGE)
    .spline(cap_all[1:], includeCurrent=True, tangents=[_unit(CAP_START_TAN), (-1.0, 0.0)],
            parameters=_chord_params(cap_all), scale=False)
    .close()
)
body = prof.revolve(360, (0, 0, 0), (0, 1, 0)).rotate((0, 0, 0), (0, 0, 1), SEAM_ANGLE)

# ================= hanging loop =================
leg_bot = KNOB_TOP_Z - 2.0     # legs run down into the knob


def _arch_solid(a, top, b, extra=0.0):
    """flat inverted-U plate: half ellipse (semi axes a, b) on straight legs, thickness LOOP_T along Y"""
    zc = top - b
    return (
        cq.Workplane("XZ", origin=(0, LOOP_T / 2.0 + extra, 0))
        .moveTo(a, leg_bot - extra)
        .lineTo(a, zc)
        .ellipseArc(a, b, 0, 180, startAtCurrent=True)
        .lineTo(-a, leg_bot - extra)
        .close()
        .extrude(LOOP_T + 2.0 * extra)
    )


loop = _arch_solid(LOOP_A_OUT, LOOP_TOP_Z, LOOP_B_OUT).cut(
    _arch_solid(LOOP_A_IN, LOOP_IN_TOP_Z, LOOP_B_IN, extra=0.5)
)

# ================= locking tabs =================
tab_in = R_SKIRT - 2.0
tabs = None
for i in range(N_TABS):
    t = (
        cq.Workplane("XY")
        .center((tab_in + TAB_OUT) / 2.0, 0)
        .box(TAB_OUT - tab_in, TAB_W, TAB_H, centered=(True, True, False))
        .rotate((0, 0, 0), (0, 0, 1), 360.0 / N_TABS * i)
    )
    tabs = t if tabs is None else tabs.union(t)

result = body.union(loop).union(tabs)

VIEW = {"azimuth": 45, "elevation": 26}
